import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 170.0            # plate width (X) at the rear, straight section
L = 233.0            # plate length (Y), flange front face -> rear edge
T = 5.0              # plate thickness
W_FRONT = 148.8      # plate / flange width at the front face
TAPER_LEN = 97.0     # length (from front face) of the tapered section

H = 30.0             # flange total height (from plate underside)
FT = 8.0             # flange thickness (Y)

GUSSET_T = 5.0       # gusset rib thickness
GUSSET_FLAT = 1.5    # short level top of the gusset behind the flange
GUSSET_RUN = 23.1    # horizontal run of the 45-ish degree gusset slope
GUSSET_TOE = 1.1     # small vertical toe at the rear end of the gusset

# front-face bosses
FB_D = 8.5           # boss diameter
FB_LEN = 4.0         # boss protrusion
FB_X = [-69.5, -35.5, 35.5, 69.5]
FB_Z_OFF = 4.7       # boss centre distance from flange top / bottom
FB_HOLE = 3.8        # through hole
FB_HOLE_EXTRA = 3.0  # holes run a little past the flange back face

# plate standoffs
SO_D = 8.0
SO_H = 5.0
SO_HOLE = 3.7
SO_POS = [
    (-78.4, 226.3), (78.4, 226.3),      # rear corners
    (-78.4, 102.9), (78.4, 102.9),      # mid sides
    (-68.3, 48.3), (-36.1, 54.0),       # front group (left pair)
    (36.3, 48.3), (68.6, 54.0),         # front group (right pair)
]

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- helpers ----------------
hw_front = W_FRONT / 2.0
hw = W / 2.0
slope = (hw - hw_front) / TAPER_LEN


def half_width(y):
    if y >= TAPER_LEN:
        return hw
    return hw_front + slope * y


# ---------------- base plate ----------------
plate_pts = [
    (-hw_front, 0.0), (hw_front, 0.0),
    (hw, TAPER_LEN), (hw, L),
    (-hw, L), (-hw, TAPER_LEN),
]
plate = cq.Workplane("XY").polyline(plate_pts).close().extrude(T)

# ---------------- front flange ----------------
fl_pts = [
    (-hw_front, 0.0), (hw_front, 0.0),
    (half_width(FT), FT), (-half_width(FT), FT),
]
flange = cq.Workplane("XY").polyline(fl_pts).close().extrude(H)
body = plate.union(flange)

# ---------------- front bosses with through holes ----------------
fb_z = [FB_Z_OFF, H - FB_Z_OFF]
boss_pts = [(x, z) for x in FB_X for z in fb_z]
# workplane on the front face, normal pointing -Y
fw = cq.Workplane("XZ", origin=(0, 0, 0))
bosses = fw.pushPoints(boss_pts).circle(FB_D / 2.0).extrude(FB_LEN)
body = body.union(bosses)

hole_wp = cq.Workplane("XZ", origin=(0, -FB_LEN, 0))
# upper row: plain through holes
upper = [(x, H - FB_Z_OFF) for x in FB_X]
thru = (
    hole_wp.pushPoints(upper)
    .circle(FB_HOLE / 2.0)
    .extrude(-(FB_LEN + FT + 1.0))
)
# lower row sits at plate-top level: the drilling runs a little past the
# flange back face and leaves a short half-groove in the plate
lower = [(x, FB_Z_OFF) for x in FB_X]
blind = (
    hole_wp.pushPoints(lower)
    .circle(FB_HOLE / 2.0)
    .extrude(-(FB_LEN + FT + FB_HOLE_EXTRA))
)
body = body.cut(thru).cut(blind)

# ---------------- gussets (follow the tapered edge) ----------------
# triangular side profile in the YZ plane, extruded across the whole width
y0 = FT
yf = FT + GUSSET_FLAT
y1 = yf + GUSSET_RUN
wedge = (
    cq.Workplane("YZ", origin=(-hw - 5, 0, 0))
    .polyline([(y0, 0.0), (y0, H), (yf, H), (y1, T + GUSSET_TOE), (y1, 0.0)])
    .close()
    .extrude(W + 10)
)
for sgn in (-1, 1):
    xa = sgn * half_width(y0)
    xb = sgn * half_width(y1)
    strip_pts = [
        (xa, y0), (xb, y1),
        (xb - sgn * GUSSET_T, y1), (xa - sgn * GUSSET_T, y0),
    ]
    strip = cq.Workplane("XY").polyline(strip_pts).close().extrude(H)
    body = body.union(strip.intersect(wedge))

# ---------------- standoffs on the plate ----------------
standoffs = (
    cq.Workplane("XY", origin=(0, 0, T))
    .pushPoints(SO_POS)
    .circle(SO_D / 2.0)
    .extrude(SO_H)
)
body = body.union(standoffs)
so_holes = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .pushPoints(SO_POS)
    .circle(SO_HOLE / 2.0)
    .extrude(T + SO_H + 2)
)
body = body.cut(so_holes)

result = body
